import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Chevron (V-shaped) open tray: flat floor + perimeter walls.  The two arms
# run at +/-45 deg from the outer apex (at the origin, pointing -Y), the arm
# ends are cut parallel to the Y axis.  Two screw holes near the top of every
# wall, and a rectangular notch cut down from the top of the inner
# (notch-side) wall of the left arm.
# ---------------------------------------------------------------------------

# ------------------------------------------------------------ driving sizes
XH = 118.5        # half of the overall X extent (arm ends at X = +/-XH)
D = 100.0         # Y distance outer apex -> inner apex (= end-wall length)
H = 45.5          # overall height
T = 6.35          # thickness of the long (diagonal) walls
T_END = 5.7       # thickness of the two end walls
F = 9.25          # floor thickness

HOLE_D = 7.0      # wall hole diameter
BLIND_DEPTH = 4.0 # depth of the one blind hole (right end wall)

# notch in the inner wall of the left arm (X range of the wall's outer face)
NOTCH_X0 = -91.5
NOTCH_X1 = -61.5
NOTCH_BOTTOM = 27.0   # Z of the notch floor

# hole layout per wall: (distance along the outer face from the wall start,
#                        centre drop below the top edge[, blind depth])
HOLES = {
    "right_outer": [(14.9, 7.0), (150.85, 7.8)],
    "left_outer": [(14.0, 6.0), (156.4, 7.9)],
    "right_end": [(9.3, 7.0), (67.6, 6.3, BLIND_DEPTH)],
    "left_end": [(9.95, 6.8), (76.35, 7.1)],
    "right_inner": [(2.7, 7.6), (137.7, 5.65)],
    "left_inner": [(2.7, 7.0), (142.0, 7.0)],
}

S2 = math.sqrt(2.0)
R2 = 1.0 / S2

# ---------------------------------------------------------------- main body
outer_pts = [
    (0.0, 0.0),
    (XH, XH),
    (XH, XH + D),
    (0.0, D),
    (-XH, XH + D),
    (-XH, XH),
]
body = cq.Workplane("XY").polyline(outer_pts).close().extrude(H)

# interior pocket = outline moved inwards by the wall thicknesses
ti = T * S2
xi = XH - T_END
inner_pts = [
    (0.0, ti),
    (xi, xi + ti),
    (xi, xi + D - ti),
    (0.0, D - ti),
    (-xi, xi + D - ti),
    (-xi, xi + ti),
]
pocket = (
    cq.Workplane("XY")
    .workplane(offset=F)
    .polyline(inner_pts)
    .close()
    .extrude(H)
)
body = body.cut(pocket)

# ---------------------------------------------------------------- wall holes
# wall frames: start point of the outer face, unit direction along the wall,
# outward unit normal
WALLS = {
    "right_outer": ((0.0, 0.0), (R2, R2), (R2, -R2)),
    "left_outer": ((0.0, 0.0), (-R2, R2), (-R2, -R2)),
    "right_end": ((XH, XH), (0.0, 1.0), (1.0, 0.0)),
    "left_end": ((-XH, XH), (0.0, 1.0), (-1.0, 0.0)),
    "right_inner": ((0.0, D), (R2, R2), (-R2, R2)),
    "left_inner": ((0.0, D), (-R2, R2), (R2, R2)),
}


def wall_hole(start, direction, normal, a, drop, depth=None):
    """Cylindrical cutter drilled from the outer face into a wall (straight
    through unless a blind depth is given)."""
    cx = start[0] + direction[0] * a
    cy = start[1] + direction[1] * a
    plane = cq.Plane(
        origin=(cx, cy, H - drop),
        xDir=(0.0, 0.0, 1.0),          # circle seam on top of the bore
        normal=(-normal[0], -normal[1], 0.0),
    )
    length = T + 3.0 if depth is None else depth
    return cq.Workplane(plane).circle(HOLE_D / 2.0).extrude(length)


for name, (start, direction, normal) in WALLS.items():
    for h in HOLES[name]:
        body = body.cut(wall_hole(start, direction, normal, *h))

# ---------------------------------------------------------------- notch
# the left-arm inner wall runs from (0, D) along (-1, 1)/sqrt2
a0 = -NOTCH_X1 * S2          # along-wall distance of the near end
a1 = -NOTCH_X0 * S2          # along-wall distance of the far end
n_len = a1 - a0
n_mid = 0.5 * (a0 + a1)
mid_x = -n_mid * R2
mid_y = D + n_mid * R2
notch_h = H - NOTCH_BOTTOM + 5.0
notch = (
    cq.Workplane("XY")
    .box(n_len, T * 4.0, notch_h)
    .rotate((0, 0, 0), (0, 0, 1), -45.0)
    .translate((mid_x, mid_y, NOTCH_BOTTOM + notch_h / 2.0))
)
body = body.cut(notch)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
